"""Teardrop-shaped housing / cable clip.

Closed front face at y=0, open stepped cavity at the back (+Y) with a spigot
lip, a steep-ramped U slot through the top of the big lobe leading into the
cavity, a rectangular side pocket at the lower front with a bore into a screw
boss, and two blind holes at the lobe centres.
"""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R = 20.0          # big lobe radius
r = 12.7          # small lobe radius
d = 23.2          # distance between lobe centres (along +X)
D_BODY = 22.05    # depth of main body (Y), closed front face at y=0
LIP_L = 1.6       # length of spigot lip at open back
LIP_IN = 0.55     # radial inset of the lip
T_WALL = 3.2      # wall thickness around the deep (front) part of the cavity
T_WALL_OUT = 2.2  # wall thickness of the rear part of the cavity
Y_LEDGE = 19.4    # y of the internal ledge where the wall steps from T_WALL to T_WALL_OUT
T_FRONT = 14.8    # thickness of the solid front block (cavity floor at y=T_FRONT)
CAV_FILLET = 0.0  # fillet between cavity floor and cavity wall (0 = sharp)
CB_WALL = 1.95    # wall thickness left at the mouth counterbore
CB_DEPTH = 1.75   # mouth counterbore depth

# top slot (plan U, vertical walls) + inner channel with ramp
SLOT_A = 5.1      # half width of slot / channel
SLOT_END = 14.56  # y of the slot's rear end on the top surface
RAMP_Z0 = 19.95   # ramp height at the front face (front face stays almost intact)
RAMP_K = 2.0      # ramp slope (drop in z per mm of y)
CH_ZC = 7.4       # centre height of the channel's round bottom

# bottom rectangular pocket (cut along -X from the small-lobe side)
PK_Y0 = 0.74
PK_Y1 = 11.87
PK_ZTOP = -9.28
PK_X0 = 6.15

# screw boss inside cavity, its bore continues into the pocket
BOSS_X = 16.8
BOSS_Z = -9.9
BOSS_OD = 5.8
BOSS_ID = 4.4
BOSS_TOP = 20.4   # y of the boss end face

HOLE_D = 4.4      # blind holes at both lobe centres in the cavity floor
HOLE_DEPTH = 4.0

VIEW = {"azimuth": 45, "elevation": 26}


def teardrop_pts(Rb, rs, dist):
    phi = math.asin((Rb - rs) / dist)
    s, c = math.sin(phi), math.cos(phi)
    ub = (Rb * s, Rb * c)
    us = (dist + rs * s, rs * c)
    ls = (dist + rs * s, -rs * c)
    lb = (Rb * s, -Rb * c)
    return ub, us, ls, lb, phi


def teardrop_wire(Rb, rs, dist):
    """Closed teardrop profile in the XZ plane (y=0): big circle Rb at the
    origin, small circle rs at x=dist, joined by the two tangent lines."""
    ub, us, ls, lb, _ = teardrop_pts(Rb, rs, dist)
    return (
        cq.Workplane("XZ")
        .moveTo(*ub)
        .lineTo(*us)
        .threePointArc((dist + rs, 0), ls)
        .lineTo(*lb)
        .threePointArc((-Rb, 0), ub)
        .close()
        .wires()
        .val()
    )


def teardrop_solid(Rb, rs, dist, y0, y1):
    """Teardrop prism (profile in XZ), spanning Y from y0 to y1 (y1>y0)."""
    w = teardrop_wire(Rb, rs, dist)
    solid = cq.Solid.extrudeLinear(w, [], cq.Vector(0, y1 - y0, 0))
    return cq.Workplane().add(solid).translate((0, y0, 0))


D_TOT = D_BODY + LIP_L

# ---- outer body with rear spigot lip ----
body = teardrop_solid(R, r, d, 0.0, D_BODY)
lip = teardrop_solid(R - LIP_IN, r - LIP_IN, d, D_BODY - 0.01, D_TOT)
part = body.union(lip)

# ---- stepped rear cavity (deep part + wider rear part) + mouth counterbore ----
Ri, ri = R - T_WALL, r - T_WALL
cav = teardrop_solid(Ri, ri, d, T_FRONT, Y_LEDGE + 0.5)  # deep part
cav_out = teardrop_solid(R - T_WALL_OUT, r - T_WALL_OUT, d, Y_LEDGE, D_TOT + 2)
if CAV_FILLET > 0:
    cav = cav.faces("<Y").edges().fillet(CAV_FILLET)
part = part.cut(cav).cut(cav_out)
cb = teardrop_solid(R - CB_WALL, r - CB_WALL, d, D_TOT - CB_DEPTH, D_TOT + 2)
part = part.cut(cb)

# ---- top slot + inner channel, both limited by a steep front ramp ----
# half-space above the ramp (z + K*y >= Z0)
ramp_ang = math.degrees(math.atan(RAMP_K))
ramp_keep = (
    cq.Workplane("XY")
    .box(40, 60, 120, centered=(True, False, True))   # y in [0,60], z in [-60,60]
    .rotate((0, 0, 0), (1, 0, 0), 90 - ramp_ang)      # tilt so its front face is the ramp
    .translate((0, 0, RAMP_Z0))
)
yc = SLOT_END - SLOT_A
slot_top = (
    cq.Workplane("XY", origin=(0, 0, Ri - 2.0))
    .moveTo(-SLOT_A, -2)
    .lineTo(SLOT_A, -2)
    .lineTo(SLOT_A, yc)
    .threePointArc((0, SLOT_END), (-SLOT_A, yc))
    .close()
    .extrude(R + 5 - (Ri - 2.0))
)
channel = (
    cq.Workplane("XZ", origin=(0, T_FRONT + 0.5, 0))
    .moveTo(-SLOT_A, R + 2)
    .lineTo(-SLOT_A, CH_ZC)
    .threePointArc((0, CH_ZC - SLOT_A), (SLOT_A, CH_ZC))
    .lineTo(SLOT_A, R + 2)
    .close()
    .extrude(T_FRONT + 2.5)
)
inner_cyl = cq.Workplane("XZ", origin=(0, T_FRONT + 2.0, 0)).circle(Ri + 0.2).extrude(T_FRONT + 4)
channel = channel.intersect(inner_cyl)
slot_cut = slot_top.union(channel).intersect(ramp_keep)
part = part.cut(slot_cut)

# ---- bottom pocket ----
pocket = cq.Workplane("XY").box(
    40, PK_Y1 - PK_Y0, 30, centered=False
).translate((PK_X0, PK_Y0, PK_ZTOP - 30))
part = part.cut(pocket)

# ---- screw boss + through bore into the pocket ----
boss = (
    cq.Workplane("XZ", origin=(0, BOSS_TOP, 0))
    .center(BOSS_X, BOSS_Z)
    .circle(BOSS_OD / 2)
    .extrude(BOSS_TOP - T_FRONT + 1)
)
part = part.union(boss)
bore = (
    cq.Workplane("XZ", origin=(0, BOSS_TOP + 1, 0))
    .center(BOSS_X, BOSS_Z)
    .circle(BOSS_ID / 2)
    .extrude(BOSS_TOP + 1 - PK_Y1 + 1)
)
part = part.cut(bore)

# ---- blind holes at the lobe centres ----
for hx in (0.0, d):
    h = (
        cq.Workplane("XZ", origin=(0, T_FRONT + 0.01, 0))
        .center(hx, 0)
        .circle(HOLE_D / 2)
        .extrude(HOLE_DEPTH)
    )
    part = part.cut(h)

result = part
